import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 11.1          # outer radius of the band
R_IN = 10.3           # inner radius of the band
WIDTH = 4.93          # band width (along Y, the ring axis)

PLAQUE_W = 2.25       # plaque width (along Y)
PLAQUE_Y = -0.13      # plaque centre offset along Y
PLAQUE_HALF_Z = 4.87  # projected half length of the plaque (outer corner, along Z)
PLAQUE_T = 0.15       # plaque raise above band surface

# lettering: each word with the Z span (top, bottom) it occupies on the plaque
WORDS = (("Death's", 4.26, 0.0), ("Storm", -0.90, -4.41))
TEXT_H = 0.15         # lettering raise above the plaque
TEXT_Y = -0.05        # lettering centre (cap-height block) along Y

RIVET_R = 0.08        # corner rivet dome radius
RIVET_INSET = 0.21    # rivet inset from plaque edges

# angular position of the cylinder seams (kept out of sight)
SEAM_OUT_DEG = 230.0
SEAM_IN_DEG = 315.0

VIEW = {"azimuth": 45, "elevation": 26}

R_PL = R_OUT + PLAQUE_T                      # plaque outer radius
THETA = math.asin(PLAQUE_HALF_Z / R_PL)      # plaque half angle


def cylinder(r, w, seam_deg, y0=0.0):
    """Solid cylinder along Y, centred at y0, with its seam at angle seam_deg
    (measured in the XZ plane from +X towards +Z)."""
    c = cq.Workplane("XZ").circle(r).extrude(w / 2.0, both=True)
    return c.rotate((0, 0, 0), (0, 1, 0), -seam_deg).translate((0, y0, 0))


def sector(r_in, r_out, half_ang, w, y0=0.0):
    """Annular sector centred on +X (radial end faces), extruded along Y."""
    c, s = math.cos(half_ang), math.sin(half_ang)
    wp = (
        cq.Workplane("XZ")
        .moveTo(r_in * c, -r_in * s)
        .lineTo(r_out * c, -r_out * s)
        .threePointArc((r_out, 0.0), (r_out * c, r_out * s))
        .lineTo(r_in * c, r_in * s)
        .threePointArc((r_in, 0.0), (r_in * c, -r_in * s))
        .close()
        .extrude(w / 2.0, both=True)
    )
    return wp.translate((0, y0, 0))


# ---------------- band ----------------
band = cylinder(R_OUT, WIDTH, SEAM_OUT_DEG).cut(
    cylinder(R_IN, WIDTH + 1.0, SEAM_IN_DEG)
)

# ---------------- plaque on +X side ----------------
plaque = sector((R_OUT + R_IN) / 2.0, R_PL, THETA, PLAQUE_W, PLAQUE_Y)

# ---------------- raised lettering ----------------
def make_text(word, size, x0, depth):
    tplane = cq.Plane(
        origin=(x0, 0.0, 0.0),
        xDir=(0, 0, -1),   # reading direction: downward on the +X face
        normal=(1, 0, 0),  # extrude outward (+X), letters' tops toward +Y
    )
    return cq.Workplane(tplane).text(
        word, size, depth, combine=False,
        font="DejaVu Serif", kind="bold",
        halign="center", valign="center",
    )


text_solid = None
try:
    x0 = R_IN - 1.5
    depth = R_PL + TEXT_H + 0.5 - x0
    # common font size: mean of the sizes that make each word fit its span
    sizes = []
    for word, z_top, z_bot in WORDS:
        sizes.append((z_top - z_bot) / make_text(word, 1.0, 0.0, 0.1).val().BoundingBox().zlen)
    size = sum(sizes) / len(sizes)
    # Y shift from the first word (all words share the same baseline)
    bb0 = make_text(WORDS[0][0], size, x0, depth).val().BoundingBox()
    dy = TEXT_Y - (bb0.ymin + bb0.ymax) / 2.0
    letters = None
    for word, z_top, z_bot in WORDS:
        w = make_text(word, size, x0, depth)
        bb = w.val().BoundingBox()
        w = w.translate((0, dy, (z_top + z_bot) / 2.0 - (bb.zmin + bb.zmax) / 2.0))
        letters = w if letters is None else letters.union(w)
    shell_txt = cylinder(R_PL + TEXT_H, PLAQUE_W, 180.0, PLAQUE_Y).cut(
        cylinder(R_PL - 0.05, PLAQUE_W + 1.0, 180.0, PLAQUE_Y)
    )
    text_solid = letters.intersect(shell_txt)
    if not text_solid.val().isValid():
        text_solid = None
except Exception:
    text_solid = None

# ---------------- corner rivets ----------------
deco = plaque
for sy in (-1, 1):
    for sz in (-1, 1):
        y = PLAQUE_Y + sy * (PLAQUE_W / 2.0 - RIVET_INSET)
        ang = sz * (THETA - RIVET_INSET / R_PL)
        x, z = R_PL * math.cos(ang), R_PL * math.sin(ang)
        dome = (
            cq.Workplane("XY")
            .sphere(RIVET_R)
            .rotate((0, 0, 0), (1, 0, 0), 90)    # poles along Y
            .rotate((0, 0, 0), (0, 1, 0), 180)   # seam buried in the plaque
            .translate((x, y, z))
        )
        deco = deco.union(dome)

if text_solid is not None:
    try:
        with_text = deco.union(text_solid)
        if with_text.val().isValid():
            deco = with_text
    except Exception:
        pass

# second plaque on -X side: same plaque turned 180 deg about the ring axis (Y)
deco2 = deco.rotate((0, 0, 0), (0, 1, 0), 180)

result = band.union(deco).union(deco2)
